import math
import cadquery as cq

# ---------------------------------------------------------------
# Caster-style kit: wheel, tube-socket hinge bracket and hinge pin
# (three separate bodies, shown in their exploded positions)
# ---------------------------------------------------------------

# ---------------- bracket (origin: back face of flange, centred) --
BOX_L = 32.5        # length of the square-tube socket along X
BOX_W = 87.5        # socket outer width (Y)
BOX_H = 83.0        # socket outer height (Z)
TUBE_W = 73.0       # socket opening width (Y)
FLOOR_STEP = 3.5    # socket floor raised above the lower arm's inner face

FL_T = 12.0         # flange thickness (X)
FL_HALF_W = 64.6    # flange half width (Y)
FL_HALF_H = 36.6    # flange half height (Z) (= top face of the arm plates)
EAR_R = 13.4        # ear corner radius (concentric with the ear holes)
EAR_HOLE_D = 11.5   # ear hole diameter
NOTCH_DEPTH = 16.2  # depth of the concave side notches (from flange side)
NOTCH_HALF = 21.6   # half height of the notches where they meet the ears

PL_T = 11.2         # arm plate thickness
TUBE_H = 2 * (FL_HALF_H - PL_T)   # socket opening height, flush with the arms
PL_END_X = 114.1    # front end of the arm plates, X
PL_TIP_R = 17.5     # radius of the rounded plate nose
PIVOT_X = 104.0     # pivot hole centre, X
PIVOT_D = 12.0      # pivot hole diameter

RIB_W = 9.5         # stiffening rib width
RIB_END_X = 94.5    # rib end, X
RIB_FILLET = 3.0    # fillet where the rib meets the socket cap

# ---------------- wheel ----------------------------------------
WHEEL_POS = (-30.8, 188.3, 123.3)
WHEEL_D = 128.0
WHEEL_W = 44.0
RIM_IN_D = 115.0    # inner diameter of the rim ring
DISH_DEPTH = 17.0   # depth of the dished face on each side
DISH_DRAFT = 3.5    # radial taper of the dish wall (moulding draft)
DISH_FILLET = 6.0
HUB_FILLET = 3.5
HUB_D = 21.6
HUB_PROJ = 7.5      # hub projection beyond the wheel faces
BORE_D = 10.0
BOLT_R = 32.0       # radius of the 3 web holes
BOLT_D = 9.5
BOLT_ANG0 = -10.0   # angle of first web hole (from +Y towards +Z)
SEAM_ANG = 55.0     # angular position of the revolve seam (cosmetic)

# ---------------- pin ------------------------------------------
PIN_POS = (0.5, -274.0)
PIN_D = 10.4
PIN_LEN = 85.5      # shank length below the head
HEAD_D = 19.8
HEAD_H = 5.0
HEAD_R = 3.8        # rounding of the head top edge
PIN_CHAMFER = 0.8
PIN_BOT_Z = -49.9


# ================================================================
def make_bracket():
    hz = BOX_H / 2.0
    hy = BOX_W / 2.0
    pad_h = hz - FL_HALF_H
    ear_y = FL_HALF_W - EAR_R
    ear_z = FL_HALF_H - EAR_R

    # --- socket block (height of the arm plates)
    box = cq.Workplane("YZ").rect(BOX_W, 2 * FL_HALF_H).extrude(BOX_L)

    # --- flange (YZ): four round ears (concentric with the bolt holes)
    #     joined by straight top/bottom edges and concave side notches
    aj = math.asin((NOTCH_HALF - ear_z) / EAR_R)      # ear/notch junction
    yj = ear_y + EAR_R * math.cos(aj)
    am = 0.5 * (math.pi / 2 + aj)                       # mid angle of ear arc
    apex = FL_HALF_W - NOTCH_DEPTH

    def ear_pt(sy, sz, a):
        return (sy * (ear_y + EAR_R * math.cos(a)), sz * (ear_z + EAR_R * math.sin(a)))

    fl = (cq.Workplane("YZ")
          .moveTo(-ear_y, FL_HALF_H)
          .lineTo(ear_y, FL_HALF_H)
          .threePointArc(ear_pt(1, 1, am), (yj, NOTCH_HALF))
          .threePointArc((apex, 0.0), (yj, -NOTCH_HALF))
          .threePointArc(ear_pt(1, -1, am), (ear_y, -FL_HALF_H))
          .lineTo(-ear_y, -FL_HALF_H)
          .threePointArc(ear_pt(-1, -1, am), (-yj, -NOTCH_HALF))
          .threePointArc((-apex, 0.0), (-yj, NOTCH_HALF))
          .threePointArc(ear_pt(-1, 1, am), (-ear_y, FL_HALF_H))
          .close()
          .extrude(FL_T))
    ear_holes = (cq.Workplane("YZ").workplane(offset=-1)
                 .pushPoints([(sy * ear_y, sz * ear_z)
                              for sy in (-1, 1) for sz in (-1, 1)])
                 .circle(EAR_HOLE_D / 2.0).extrude(FL_T + 2))
    fl = fl.cut(ear_holes)

    body = box.union(fl)
    # --- triangular arm plates: tangent lines from the socket corners
    #     to the rounded tip around the pivot hole
    tip_c = PL_END_X - PL_TIP_R
    dist = math.hypot(tip_c - BOX_L, hy)
    beta = math.acos(PL_TIP_R / dist)
    ang_c = math.atan2(hy, BOX_L - tip_c)
    t1 = (tip_c + PL_TIP_R * math.cos(ang_c - beta),
          PL_TIP_R * math.sin(ang_c - beta))
    t2 = (t1[0], -t1[1])

    def plate(z0):
        return (cq.Workplane("XY").workplane(offset=z0)
                .moveTo(BOX_L - 1.0, hy)
                .lineTo(BOX_L, hy)
                .lineTo(t1[0], t1[1])
                .threePointArc((PL_END_X, 0.0), t2)
                .lineTo(BOX_L, -hy)
                .lineTo(BOX_L - 1.0, -hy)
                .close()
                .extrude(PL_T))

    body = body.union(plate(FL_HALF_H - PL_T)).union(plate(-FL_HALF_H))

    # --- socket opening through everything
    opening = (cq.Workplane("YZ").workplane(offset=-1.0)
               .center(0, FLOOR_STEP / 2.0)
               .rect(TUBE_W, TUBE_H - FLOOR_STEP).extrude(BOX_L + 2.0))
    body = body.cut(opening)

    # --- pivot holes
    piv = (cq.Workplane("XY").workplane(offset=-hz - 1)
           .center(PIVOT_X, 0).circle(PIVOT_D / 2.0).extrude(BOX_H + 2))
    body = body.cut(piv)

    # --- T-shaped pads on top and bottom: socket cap + stiffening rib,
    #     with rounded inner corners where the rib leaves the cap
    rw = RIB_W / 2.0
    for sz in (1, -1):
        z0 = FL_HALF_H if sz > 0 else -hz
        pad = (cq.Workplane("XY").workplane(offset=z0)
               .moveTo(0, -hy).lineTo(BOX_L, -hy).lineTo(BOX_L, -rw)
               .lineTo(RIB_END_X, -rw).lineTo(RIB_END_X, rw)
               .lineTo(BOX_L, rw).lineTo(BOX_L, hy).lineTo(0, hy).close()
               .extrude(pad_h))
        pad = pad.edges("|Z").edges(
            cq.selectors.BoxSelector((BOX_L - 0.1, -rw - 0.1, -100),
                                     (BOX_L + 0.1, rw + 0.1, 100))
        ).fillet(RIB_FILLET)
        # keep the seam between cap and socket walls (separate faces)
        body = body.union(pad, clean=False)
    return body


def make_wheel():
    r = WHEEL_D / 2.0
    hw = WHEEL_W / 2.0
    rin = RIM_IN_D / 2.0
    rh = HUB_D / 2.0
    web = hw - DISH_DEPTH
    hub_end = hw + HUB_PROJ
    # half profile in the XY plane (Y = radius), revolved about X
    pts = [
        (-hub_end, BORE_D / 2.0),
        (-hub_end, rh),
        (-web, rh),
        (-web, rin - DISH_DRAFT),
        (-hw, rin),
        (-hw, r),
        (hw, r),
        (hw, rin),
        (web, rin - DISH_DRAFT),
        (web, rh),
        (hub_end, rh),
        (hub_end, BORE_D / 2.0),
    ]
    wheel = (cq.Workplane("XY").polyline(pts).close()
             .revolve(360.0, (0, 0, 0), (1, 0, 0)))

    class _CircleAt(cq.Selector):
        """circular edges lying in the plane X = x with radius rad"""

        def __init__(self, x, rad):
            self.x, self.rad = x, rad

        def filter(self, objs):
            out = []
            for e in objs:
                bb = e.BoundingBox()
                if abs(bb.xmin - self.x) < 0.3 and abs(bb.xmax - self.x) < 0.3 \
                        and abs(bb.ymax - self.rad) < 0.3:
                    out.append(e)
            return out

    def sel_circle(x, rad):
        return _CircleAt(x, rad)

    for sx in (-1, 1):
        wheel = wheel.edges(sel_circle(sx * web, rin - DISH_DRAFT)).fillet(DISH_FILLET)
        wheel = wheel.edges(sel_circle(sx * web, rh)).fillet(HUB_FILLET)
    # turn the revolve seam towards the silhouette of the main view
    wheel = wheel.rotate((0, 0, 0), (1, 0, 0), SEAM_ANG)
    # three through holes in the web
    for k in range(3):
        a = math.radians(BOLT_ANG0 + 120.0 * k)
        h = (cq.Workplane("YZ").workplane(offset=-hw)
             .center(BOLT_R * math.cos(a), BOLT_R * math.sin(a))
             .circle(BOLT_D / 2.0).extrude(WHEEL_W))
        wheel = wheel.cut(h)
    return wheel.translate(WHEEL_POS)


def make_pin():
    rs = PIN_D / 2.0
    rh = HEAD_D / 2.0
    # shank (seam placed on the side facing away from the main view)
    shank_pl = cq.Plane(origin=(0, 0, 0), xDir=(1, 1, 0), normal=(0, 0, 1))
    shank = (cq.Workplane(shank_pl).circle(rs).extrude(PIN_LEN)
             .faces("<Z").chamfer(PIN_CHAMFER))
    # button head: short cylinder with a well rounded top edge
    head_pl = cq.Plane(origin=(0, 0, PIN_LEN), xDir=(0, -1, 0), normal=(0, 0, 1))
    head = (cq.Workplane(head_pl).circle(rh).extrude(HEAD_H)
            .faces(">Z").edges().fillet(HEAD_R))
    pin = shank.union(head)
    # flat on the head, flush with the shank on the -Y side
    cutter = (cq.Workplane("XY").box(40, 40, 40)
              .translate((0, -rs - 20.0, PIN_LEN + 20.0 - 0.01)))
    pin = pin.cut(cutter)
    return pin.translate((PIN_POS[0], PIN_POS[1], PIN_BOT_Z))


bracket = make_bracket()
wheel = make_wheel()
pin = make_pin()

result = bracket.union(wheel, clean=False).union(pin, clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
